import cadquery as cq
import math

# ---------------- driving dimensions (mm) ----------------
L = 120.0            # overall length (Y)
W = 83.2             # overall width at the side bulges (X)
H_BODY = 25.1        # height of main wall body
LIP_H = 2.1          # raised inner lip on top of the wall
BOT_CH = 1.9         # chamfer around the bottom edge

SIDE_INSET = 2.3     # corner sections of the long sides are inset by this
CORNER_CH = 5.3      # 45 deg vertical corner chamfer
SIDE_FLAT = 10.9     # flat length of long side between corner chamfer and step

NOTCH_D = 5.2        # depth of the recess in the middle of each end face
NOTCH_IN = 14.8      # half width of recessed end face
NOTCH_OUT = 18.9     # half width of recess opening at the outer face

WALL = 3.15          # end wall thickness
WALL_SIDE_C = 3.5    # long side wall thickness at the corner sections
WALL_SIDE_M = 4.2    # long side wall thickness at the middle bulge
LIP_INSET = 1.55     # outer ledge width below the lip
FLOOR = 2.2          # floor thickness

# corner screw bosses
HOLE_X = 31.4
HOLE_Y = 55.7
HOLE_D = 4.2
BOSS_R = 4.2
NUT_AF = 7.5
NUT_DEPTH = 4.2

# PCB standoffs (x, y, body diameter)
STANDOFFS = [(-17.7, 43.6, 4.7), (26.0, 43.6, 4.7),
             (-26.1, -19.4, 6.4), (26.0, -20.5, 6.4)]
SO_TOP = 18.2
PIN_D = 3.4
PIN_TOP = 20.2
PIN_HOLE_D = 1.0
SO_FILLET = 3.6

# cable hole in the +Y end wall with square seat pocket on the inside
CH_X = 8.5
CH_Z = 19.5
CH_D = 6.5
SEAT = 11.2
SEAT_DEPTH = 0.8
SEAT_X = 8.25
SEAT_Z = 19.3

hl = L / 2.0
hw = W / 2.0
hwc = hw - SIDE_INSET
y_step0 = hl - CORNER_CH - SIDE_FLAT


def outline_pts(hw, hwc):
    step = hw - hwc
    q = [  # one quadrant (x>=0, y<=0), from the middle of the -Y end to the middle of +X side
        (NOTCH_IN, -hl + NOTCH_D),
        (NOTCH_OUT, -hl),
        (hwc - CORNER_CH, -hl),
        (hwc, -hl + CORNER_CH),
        (hwc, -y_step0),
        (hw, -(y_step0 - step)),
    ]
    # build full loop counter-clockwise
    pts = []
    # bottom side (y<0) from left to right
    for (x, y) in reversed(q):
        pts.append((-x, y))
    for (x, y) in q:
        pts.append((x, y))
    # top side (y>0) from right to left
    for (x, y) in reversed(q):
        pts.append((x, -y))
    for (x, y) in q:
        pts.append((-x, -y))
    return pts


def prism(wire, z0, z1):
    face = cq.Face.makeFromWires(wire)
    return cq.Workplane("XY").add(cq.Solid.extrudeLinear(face, cq.Vector(0, 0, z1 - z0))
                                  .translate(cq.Vector(0, 0, z0)))


def poly_wire(pts):
    return cq.Wire.makePolygon([cq.Vector(x, y, 0) for x, y in pts], close=True)


outer_wire = poly_wire(outline_pts(hw, hwc))
lip_wire = outer_wire.offset2D(-LIP_INSET, kind="intersection")[0]
# cavity: offset of an outline whose long sides are pulled in so that the
# side walls come out thicker than the end walls
cav_base = poly_wire(outline_pts(hw - (WALL_SIDE_M - WALL), hwc - (WALL_SIDE_C - WALL)))
cav_wire = cav_base.offset2D(-WALL, kind="intersection")[0]

# main body with bottom chamfer
body = prism(outer_wire, 0, H_BODY)
body = body.faces("<Z").edges().chamfer(BOT_CH)
# raised lip
body = body.union(prism(lip_wire, H_BODY - 0.01, H_BODY + LIP_H))

# cavity minus the four corner screw bosses
TOP = H_BODY + LIP_H
cavity = prism(cav_wire, FLOOR, TOP + 1.0)
for sx in (-1, 1):
    for sy in (-1, 1):
        cx, cy = sx * HOLE_X, sy * HOLE_Y
        boss = (cq.Workplane("XY").workplane(offset=FLOOR - 1)
                .center(cx, cy).circle(BOSS_R).extrude(TOP + 3 - FLOOR))
        # rectangles filling the space between the round boss and the corner walls
        r1 = (cq.Workplane("XY").workplane(offset=FLOOR - 1)
              .center(cx + sx * (12.0 - BOSS_R) / 2, cy + sy * 6.0)
              .rect(12.0 + BOSS_R, 12.0).extrude(TOP + 3 - FLOOR))
        r2 = (cq.Workplane("XY").workplane(offset=FLOOR - 1)
              .center(cx + sx * 6.0, cy + sy * (12.0 - BOSS_R) / 2)
              .rect(12.0, 12.0 + BOSS_R).extrude(TOP + 3 - FLOOR))
        cavity = cavity.cut(boss).cut(r1).cut(r2)

body = body.cut(cavity)

# screw holes through the bosses and hex nut traps underneath
for sx in (-1, 1):
    for sy in (-1, 1):
        cx, cy = sx * HOLE_X, sy * HOLE_Y
        hole = cq.Workplane("XY").workplane(offset=-1).center(cx, cy).circle(HOLE_D / 2).extrude(TOP + 2)
        nut = (cq.Workplane("XY").workplane(offset=-1).center(cx, cy)
               .polygon(6, NUT_AF / math.cos(math.radians(30))).extrude(NUT_DEPTH + 1))
        body = body.cut(hole).cut(nut)

# PCB standoffs with base fillet and locating pin
for (sx, sy, d) in STANDOFFS:
    so = (cq.Workplane("XY").workplane(offset=FLOOR - 0.5).center(sx, sy)
          .circle(d / 2).extrude(SO_TOP - FLOOR + 0.5))
    body = body.union(so)
    # fillet at the base where it meets the floor
    try:
        body = body.edges(cq.selectors.BoxSelector((sx - d, sy - d, FLOOR - 0.01),
                                                   (sx + d, sy + d, FLOOR + 0.01))).fillet(SO_FILLET)
    except Exception:
        pass
    pin = (cq.Workplane("XY").workplane(offset=SO_TOP - 0.01).center(sx, sy)
           .circle(PIN_D / 2).extrude(PIN_TOP - SO_TOP + 0.01))
    body = body.union(pin)
    ph = (cq.Workplane("XY").workplane(offset=PIN_TOP - 4.0).center(sx, sy)
          .circle(PIN_HOLE_D / 2).extrude(5.0))
    body = body.cut(ph)

# cable entry hole in the +Y end wall with a shallow square seat on the inside
y_in = hl - NOTCH_D - WALL
seat = (cq.Workplane("XZ", origin=(0, y_in - 0.5, 0)).center(SEAT_X, SEAT_Z)
        .rect(SEAT, SEAT).extrude(-(SEAT_DEPTH + 0.5)))
body = body.cut(seat)
chole = (cq.Workplane("XZ", origin=(0, y_in - 1.0, 0)).center(CH_X, CH_Z)
         .circle(CH_D / 2).extrude(-(WALL + 8.0)))
body = body.cut(chole)

result = body
